import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Mask ear-saver strap: flat plate in the XZ plane, hook heads at both ends,
# oval ring in the middle, raised ribs on the back (+Y) of the hook heads.
# ---------------------------------------------------------------------------

# --- driving dimensions (mm) ---
THETA = 8.0          # arm tilt (outer ends lower), degrees
W = 6.37             # strip half width
RING_A = 25.5        # ring outer ellipse half length (X)
RING_B = 14.3        # ring outer ellipse half height (Z)
RING_DZ = 0.3        # ring / hole centre above the arm axes crossing
HOLE_A = 17.4        # oval hole half length
HOLE_B = 6.37        # oval hole half height
JUNC_R_TOP = 5.5     # fillet ring <-> strip, upper edge
JUNC_R_BOT = 3.0     # fillet ring <-> strip, lower edge

N_TEETH = 4          # hooks per side per head
U1 = 40.5            # first bulb centre along arm (from centre)
PITCH = 10.1         # hook pitch along the arm
VB = 12.6            # bulb centre distance from arm axis
RB = 2.5             # bulb radius
DI = 0.6             # inner finger edge offset from bulb centre
RN = 1.0             # notch fillet under bulb
RC = 1.1             # slot-bottom fillet
PHI = 61.0           # slant of outer finger edge relative to arm axis (deg)
U_END = 77.4         # end face position along arm (on the axis)
R_END = 50.0         # radius of the slightly convex end face
R_COR = 3.5          # corner rounding between slant and end face

T_PLATE = 1.2        # plate thickness
T_RIB = 1.15         # rib height above the plate (back side)
RIB_FILLET = 1.12    # rounding of rib back edges
PLATE_FILLET = 0.6   # rounding of plate back edges
GROOVE_EXTRA = 0.4   # widen grooves toward the outer tooth edge

VIEW = {"azimuth": 45, "elevation": 26}


# ---------------------------------------------------------------------------
# 2D helpers (arm local coords: u along arm outward, v perpendicular)
# ---------------------------------------------------------------------------
def _add(a, b):
    return (a[0] + b[0], a[1] + b[1])


def _sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def _mul(a, s):
    return (a[0] * s, a[1] * s)


def _norm(a):
    l = math.hypot(a[0], a[1])
    return (a[0] / l, a[1] / l)


def _ang(a):
    return math.atan2(a[1], a[0])


def _pt(c, r, ang):
    return (c[0] + r * math.cos(ang), c[1] + r * math.sin(ang))


def corner_fillet(p_prev, p, p_next, r):
    """Fillet between segment p_prev->p and p->p_next. Returns (t1, mid, t2)."""
    d1 = _norm(_sub(p, p_prev))
    d2 = _norm(_sub(p_next, p))
    cross = d1[0] * d2[1] - d1[1] * d2[0]
    dot = d1[0] * d2[0] + d1[1] * d2[1]
    turn = math.atan2(cross, dot)
    tl = r * math.tan(abs(turn) / 2.0)
    t1 = _sub(p, _mul(d1, tl))
    t2 = _add(p, _mul(d2, tl))
    # centre lies to the left for a left turn, to the right for a right turn
    if turn > 0:
        nrm = (-d1[1], d1[0])
    else:
        nrm = (d1[1], -d1[0])
    c = _add(t1, _mul(nrm, r))
    bis = _norm(_add(_sub(t1, c), _sub(t2, c)))
    mid = _add(c, _mul(bis, r))
    return t1, mid, t2


def top_edge_path():
    """Segments of the top edge of the right arm, u increasing."""
    segs = []
    phi = math.radians(PHI)
    n_out = (math.sin(phi), math.cos(phi))      # outward normal of slant
    d_sl = (math.cos(phi), -math.sin(phi))      # slant direction (going down)
    cur = (0.0, W)
    for k in range(N_TEETH):
        ub = U1 + k * PITCH
        C = (ub, VB)
        ui = ub - DI
        # base concave corner (horizontal -> vertical up)
        corner = (ui, W)
        t1, mid, t2 = corner_fillet(_sub(corner, (5.0, 0.0)), corner,
                                    _add(corner, (0.0, 5.0)), RC)
        segs.append(("line", cur, t1))
        segs.append(("arc", t1, mid, t2))
        # notch fillet centre F (outside material, left of the inner edge)
        fu = ui - RN
        fv = VB - math.sqrt((RB + RN) ** 2 - (DI + RN) ** 2)
        F = (fu, fv)
        n1 = (ui, fv)
        n2 = _add(C, _mul(_sub(F, C), RB / (RB + RN)))
        segs.append(("line", t2, n1))
        nb = _norm(_add(_sub(n1, F), _sub(n2, F)))
        segs.append(("arc", n1, _add(F, _mul(nb, RN)), n2))
        # bulb arc, clockwise from n2 to tangent point T
        a2 = _ang(_sub(n2, C))
        aT = _ang(n_out)
        sweep = (a2 - aT) % (2 * math.pi)
        amid = a2 - sweep / 2.0
        T = _pt(C, RB, aT)
        segs.append(("arc", n2, _pt(C, RB, amid), T))
        if k < N_TEETH - 1:
            # slant down to slot bottom
            t = (T[1] - W) / math.sin(phi)
            S = _add(T, _mul(d_sl, t))
            s1, smid, s2 = corner_fillet(T, S, _add(S, (5.0, 0.0)), RC)
            segs.append(("line", T, s1))
            segs.append(("arc", s1, smid, s2))
            cur = s2
        else:
            # slant down, round corner, then a gently curved end face
            # through (U_END, 0) (centre of the end arc on the arm axis)
            Qe = (U_END - R_END, 0.0)
            sp, cp = math.sin(phi), math.cos(phi)
            # corner circle centre K: distance RB - R_COR inside the slant
            # line and internally tangent to the end arc
            # ku = a0 + a1 * kv
            a0 = ub + (RB - R_COR + VB * cp) / sp
            a1 = -cp / sp
            bu = a0 - Qe[0]
            qa = a1 * a1 + 1.0
            qb = 2.0 * a1 * bu
            qc = bu * bu - (R_END - R_COR) ** 2
            kv = (-qb - math.sqrt(qb * qb - 4 * qa * qc)) / (2 * qa)
            K = (a0 + a1 * kv, kv)
            P1 = _add(K, _mul(n_out, R_COR))
            ke = _norm(_sub(K, Qe))
            P2 = _add(Qe, _mul(ke, R_END))
            segs.append(("line", T, P1))
            a_p1 = aT
            a_p2 = _ang(ke)
            segs.append(("arc", P1, _pt(K, R_COR, (a_p1 + a_p2) / 2.0), P2))
            segs.append(("arc", P2, _pt(Qe, R_END, a_p2 / 2.0), (U_END, 0.0)))
    return segs


def arm_face(sign):
    """Closed arm outline (strip + hook head) as a cq.Face, in global XZ.

    sign = +1 right arm, -1 left arm."""
    top = top_edge_path()
    bot = []
    for s in reversed(top):
        if s[0] == "line":
            bot.append(("line", (s[2][0], -s[2][1]), (s[1][0], -s[1][1])))
        else:
            bot.append(("arc", (s[3][0], -s[3][1]), (s[2][0], -s[2][1]),
                        (s[1][0], -s[1][1])))
    segs = top + bot
    # close back along u = 0
    segs.append(("line", (0.0, -W), (0.0, W)))

    th = math.radians(THETA)
    cu, su = math.cos(th), math.sin(th)

    def g(p):
        u, v = p
        x = u * cu + v * su
        z = -u * su + v * cu
        return cq.Vector(sign * x, 0.0, z)

    edges = []
    for s in segs:
        if s[0] == "line":
            if math.hypot(s[2][0] - s[1][0], s[2][1] - s[1][1]) < 1e-6:
                continue
            edges.append(cq.Edge.makeLine(g(s[1]), g(s[2])))
        else:
            edges.append(cq.Edge.makeThreePointArc(g(s[1]), g(s[2]), g(s[3])))
    wire = cq.Wire.assembleEdges(edges)
    return cq.Face.makeFromWires(wire)


def ellipse_face(a, b):
    e = cq.Edge.makeEllipse(a, b, pnt=cq.Vector(0, 0, RING_DZ), dir=cq.Vector(0, -1, 0),
                            xdir=cq.Vector(1, 0, 0))
    return cq.Face.makeFromWires(cq.Wire.assembleEdges([e]))


T_TOTAL = T_PLATE + T_RIB
th = math.radians(THETA)
phi = math.radians(PHI)


def outline_solid(depth):
    """Full part outline (ring + both arms) extruded from y=0 to y=depth."""
    ext = cq.Vector(0, depth, 0)
    ring = cq.Solid.extrudeLinear(ellipse_face(RING_A, RING_B), ext)
    arm_r = cq.Solid.extrudeLinear(arm_face(+1), ext)
    arm_l = cq.Solid.extrudeLinear(arm_face(-1), ext)
    s = ring.fuse(arm_r).fuse(arm_l).clean()
    # concave fillets where the strips run into the ring
    jtop, jbot = [], []
    for e in s.Edges():
        d = e.tangentAt(0.5)
        if abs(abs(d.y) - 1.0) < 1e-6 and abs(e.Center().x) < RING_A + 1.0:
            (jtop if e.Center().z > 0 else jbot).append(e)
    s = s.fillet(JUNC_R_TOP, jtop)
    return s.fillet(JUNC_R_BOT, jbot)


def _loc(sign, u, v):
    x = u * math.cos(th) + v * math.sin(th)
    z = -u * math.sin(th) + v * math.cos(th)
    return (sign * x, z)


def back_edges(shape, y, tol=1e-4):
    out = []
    for e in shape.Edges():
        bb = e.BoundingBox()
        if abs(bb.ymin - y) < tol and abs(bb.ymax - y) < tol:
            out.append(e)
    return out


# --- thin plate (outer back edges rounded) with the oval hole ---
plate = outline_solid(T_PLATE)
try:
    plate = plate.fillet(PLATE_FILLET, back_edges(plate, T_PLATE))
except Exception:
    pass
hole = cq.Solid.extrudeLinear(ellipse_face(HOLE_A, HOLE_B),
                              cq.Vector(0, T_TOTAL + 2.0, 0)).translate(
    cq.Vector(0, -1.0, 0))
plate = plate.cut(hole)

# --- raised rib columns on the back of each hook head ---
full = outline_solid(T_TOTAL)
H_G = W + RC + 0.2              # grooves run across the body up to here
u_in = U1 - DI                  # inner wall of the innermost rib
u_a = U1 - RB - 0.3             # keep the whole innermost bulb thick
u_e = U_END + 5.0
BIGV = 30.0


def prism(sign, pts_uv, y0, y1):
    pts = [_loc(sign, u, v) for (u, v) in pts_uv]
    wp = cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close()
    return wp.extrude(y1 - y0).val()


body = plate
for sign in (+1, -1):
    zone = prism(sign, [(u_in, -H_G), (u_in, H_G), (u_a, H_G), (u_a, BIGV),
                        (u_e, BIGV), (u_e, -BIGV), (u_a, -BIGV), (u_a, -H_G)],
                 -1.0, T_TOTAL + 1.0)
    thick = full.intersect(zone)
    for k in range(N_TEETH - 1):
        ub = U1 + k * PITCH
        # where the slanted outer edge of tooth k meets the strip edge
        tu = ub + RB * math.sin(phi)
        tv = VB + RB * math.cos(phi)
        g0 = tu + (tv - W) / math.tan(phi) - GROOVE_EXTRA
        g1 = U1 + (k + 1) * PITCH - DI
        groove = prism(sign, [(g0, -H_G), (g0, H_G), (g1, H_G), (g1, -H_G)],
                       T_PLATE, T_TOTAL + 1.0)
        thick = thick.cut(groove)
    for rib in thick.Solids():
        try:
            rib = rib.fillet(RIB_FILLET, back_edges(rib, T_TOTAL))
        except Exception:
            pass
        body = body.fuse(rib)
body = body.clean()

result = cq.Workplane("XY").add(body)
